import math
import cadquery as cq

# ------------------------------------------------------------------
# Two-piece clamshell battery case, printed flat: deep tray (front, -Y)
# and shallow lid (back, +Y) joined by a small hinge strap at the -X end.
# ------------------------------------------------------------------
L = 80.0            # overall length along X

# ---- tray (front half) ----
T_W = 24.6          # width
T_H = 13.3          # height
T_R = 8.0           # bottom corner radius of the D profile
T_Y = -13.26        # centre line Y
T_T = 1.3           # shell thickness (floor / lower walls)
T_OPEN = 9.47       # half width of the top opening
BORE_R = 10.7       # battery bore radius (overhanging the opening)
T_END0 = 3.3        # -X end wall thickness
T_END1 = 1.7        # +X end wall thickness
BOX_X = 10.5        # end pocket (flat walls) runs from end wall to here
NARROW_X = 54.4     # contact zone with flat walls starts here
NARROW_HW = 7.78    # half width of the contact zone
STEP_X0, STEP_HW, STEP_D = 1.38, 7.73, 1.2   # seat recess on top of the -X end wall
LATCH_X0, LATCH_X1 = 56.4, 77.8   # snap recesses on both long sides
LATCH_D = 2.7       # recess depth into wall
LATCH_H = 4.6       # recess height from top
BEAD_R, BEAD_H, BEAD_Z = 2.0, 0.6, 11.1   # snap bead in the recess
POST_XS = ((66.4, 68.6), (70.3, 72.3))   # square posts (X ranges)
POST_P = 1.45       # square post protrusion from the wall
POST_DROP = 1.4     # square post top below the rim
RIB_X, RIB_R, RIB_P = 69.5, 0.7, 2.4      # round rib position, radius, protrusion
NOTCH_HW = 5.7      # +X end wall U-notch half width
NOTCH_D = 5.8       # U-notch depth
NOTCH_C = 1.6       # U-notch bottom chamfer
NOTCH_CH = 1.0      # chamfer around the U-notch at the end face
EDGE_R = 0.8        # rounding of the tray end faces
PLAN_R = 1.0        # plan-view rounding of the tray corners
T_TOP_IN = 1.0      # top outer edge rounding (inset at the rim)
T_TOP_DROP = 2.3    # top outer edge rounding (height)

# ---- lid (back half) ----
L_Y = 12.68         # centre line Y
L_HW = 12.73        # half width of the lid profile (flange tops)
L_R = 7.5           # bottom corner radius of the lid profile
L_T = 1.6           # shell thickness
L_IN_R = 0.8        # inner corner rounding at the cavity ends
L_RIM = 3.5         # rim height
L_FL = 7.2          # flange top height
L_X1 = 78.0         # end of lid cavity / start of +X end wall
L_XE = 80.2         # end of lid
L_EDGE_R = 1.2      # rounding of the lid end faces
FL_X0, FL_X1 = 56.7, 77.6   # snap flanges
FL_W = 2.9          # flange width at top
GROOVE_R, GROOVE_D, GROOVE_Z = 2.29, 0.56, 5.7   # concave groove in flange
L_END0 = 3.4        # -X end wall thickness
L_END_THIN, L_END_HW = 1.75, 5.0   # thinner middle part of the -X end wall
LEDGE_X1, LEDGE_IN, LEDGE_OUT, LEDGE_Z = 9.8, 7.78, 9.5, 4.87   # raised ledges next to the -X end wall
PART_X0, PART_X1 = 39.0, 41.0      # partition
BLK_X0, BLK_X1, BLK_Y0, BLK_Y1, BLK_Z = 66.3, 72.2, 6.2, 7.9, 3.4   # small floor blocks
EW_BLK_HW, EW_BLK_Z, EW_BLK_CH = 6.0, 4.7, 0.8   # raised hooks on the +X end wall
EW_RAMP_X0, EW_RAMP_X1, EW_RAMP_Z = 78.4, 79.5, 4.1   # lead-in ramp of the hooks
CH_HW, CH_X0 = 1.55, 76.5   # half width / start of the channel through the +X end wall
SLOT_X0, SLOT_X1, SLOT_HW = 58.5, 72.2, 2.3   # through slot in the lid floor
HOLE_X, HOLE_D = 55.2, 1.8                     # small through hole

# ---- hinge strap ----
HINGE_X0, HINGE_X1 = 1.3, 4.6
HINGE_Y, HINGE_Z = -0.62, 3.35
HINGE_A, HINGE_B = 2.4, 0.8


# ------------------------------------------------------------------
def d_prism(x0, x1, yc, hw, h, r, z0=0.0, fillet_ends=0.0, ends="<X or >X"):
    """Prism along X with a flat top and rounded bottom corners."""
    b = cq.Workplane("XY").box(x1 - x0, 2 * hw, h).translate(((x0 + x1) / 2, yc, z0 + h / 2))
    b = b.edges("|X and <Z").fillet(r)
    if fillet_ends > 0:
        b = b.faces(ends).edges("not(>Z)").fillet(fillet_ends)
    return b


def top_round_cutter(x0, x1, yc, hw, h, top_in, top_drop):
    """Removes the outer top corners of the tray along X (arc tangent to the side wall)."""
    rho = (top_in ** 2 + top_drop ** 2) / (2 * top_in)
    ang = math.atan2(top_drop, rho - top_in) / 2.0
    mx = hw - rho + rho * math.cos(ang)
    mz = h - top_drop + rho * math.sin(ang)
    out = None
    for sg in (-1, 1):
        w = (cq.Workplane("YZ").workplane(offset=x0)
             .moveTo(yc + sg * (hw - top_in), h)
             .threePointArc((yc + sg * mx, mz), (yc + sg * hw, h - top_drop))
             .lineTo(yc + sg * (hw + 2), h - top_drop)
             .lineTo(yc + sg * (hw + 2), h + 2)
             .lineTo(yc + sg * (hw - top_in), h + 2)
             .close())
        c = w.extrude(x1 - x0)
        out = c if out is None else out.union(c)
    return out


def box(x0, x1, y0, y1, z0, z1):
    x0, x1 = sorted((x0, x1))
    y0, y1 = sorted((y0, y1))
    z0, z1 = sorted((z0, z1))
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0).translate(
        ((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2))


def cyl_x(x0, x1, y, z, r):
    return cq.Workplane("YZ").workplane(offset=x0).center(y, z).circle(r).extrude(x1 - x0)


def notch_wire(x, grow):
    nh, nd, nc = NOTCH_HW + grow, NOTCH_D + grow, NOTCH_C + grow * 0.414
    pts = [(T_Y - nh, T_H + 2), (T_Y - nh, T_H - nd + nc), (T_Y - nh + nc, T_H - nd),
           (T_Y + nh - nc, T_H - nd), (T_Y + nh, T_H - nd + nc), (T_Y + nh, T_H + 2)]
    return cq.Wire.makePolygon([cq.Vector(x, y, z) for (y, z) in pts], close=True)


# ================= TRAY =================
tray = d_prism(0, L, T_Y, T_W / 2, T_H, T_R)
tray = tray.cut(top_round_cutter(-1, L + 1, T_Y, T_W / 2, T_H, T_TOP_IN, T_TOP_DROP))
tray = tray.intersect(box(0, L, T_Y - T_W / 2, T_Y + T_W / 2, -1, T_H + 1).edges("|Z").fillet(PLAN_R))
tray = tray.faces("<X or >X").edges("not(>Z)").fillet(EDGE_R)
envelope = d_prism(0, L, T_Y, T_W / 2, T_H, T_R)

# battery bore: circle overhanging the opening, clipped by the offset shell
bore_zc = T_H - math.sqrt(BORE_R ** 2 - T_OPEN ** 2)
cav_x0, cav_x1 = T_END0, L - T_END1
inner = d_prism(cav_x0, cav_x1, T_Y, T_W / 2 - T_T, T_H + 2, T_R - T_T, z0=T_T)
cav = inner.intersect(cyl_x(cav_x0, cav_x1, T_Y, bore_zc, BORE_R))
cav = cav.union(box(cav_x0, cav_x1, T_Y - T_OPEN, T_Y + T_OPEN, bore_zc, T_H + 1).intersect(inner))
# flat walls in the -X end pocket and in the +X contact zone
keep = (box(cav_x0, BOX_X, T_Y - T_OPEN, T_Y + T_OPEN, -1, T_H + 2)
        .union(box(BOX_X, NARROW_X, T_Y - 20, T_Y + 20, -1, T_H + 2))
        .union(box(NARROW_X, cav_x1, T_Y - NARROW_HW, T_Y + NARROW_HW, -1, T_H + 2)))
tray = tray.cut(cav.intersect(keep))

# seat recess on top of the -X end wall
tray = tray.cut(box(STEP_X0, T_END0 + 0.01, T_Y - STEP_HW, T_Y + STEP_HW, T_H - STEP_D, T_H + 1))

# U notch in the +X end wall, chamfered at the end face
notch = cq.Solid.makeLoft([notch_wire(L - T_END1 - 0.5, 0.0), notch_wire(L - NOTCH_CH, 0.0)], True)
notch_ch = cq.Solid.makeLoft([notch_wire(L - NOTCH_CH, 0.0), notch_wire(L + 0.01, NOTCH_CH + 0.01)], True)
tray = tray.cut(cq.Workplane("XY").add(notch)).cut(cq.Workplane("XY").add(notch_ch))

# contact plate posts on both walls of the contact zone: two square posts and a round rib
for s in (-1, 1):
    yw = T_Y + s * NARROW_HW
    for (px0, px1) in POST_XS:
        p = box(px0, px1, yw - s * POST_P, yw + s * 0.6, 1.0, T_H - POST_DROP)
        tray = tray.union(p.intersect(envelope))
    yc = yw - s * (RIB_P - RIB_R)
    rib = box(RIB_X - RIB_R, RIB_X + RIB_R, yw + s * 0.6, yc, 1.0, T_H)
    rib = rib.union(cq.Workplane("XY").center(RIB_X, yc).circle(RIB_R).extrude(T_H - 1.0)
                    .translate((0, 0, 1.0)))
    tray = tray.union(rib.intersect(envelope))

# snap recesses on both long sides with a rounded bead
for s in (-1, 1):
    yo = T_Y + s * T_W / 2
    yin = yo - s * LATCH_D
    rec = box(LATCH_X0, LATCH_X1, yin, yo + s * 1.0, T_H - LATCH_H, T_H + 1)
    tray = tray.cut(rec)
    bead = cyl_x(LATCH_X0, LATCH_X1, yin - s * (BEAD_R - BEAD_H), BEAD_Z, BEAD_R)
    tray = tray.union(bead.intersect(rec))

# ================= LID =================
lid_env = d_prism(0, L_XE, L_Y, L_HW, L_R + 1.5, L_R)
lid = d_prism(0, L_XE, L_Y, L_HW, L_R + 1.5, L_R, fillet_ends=L_EDGE_R)
lid = lid.cut(box(-1, L_XE + 1, L_Y - 20, L_Y + 20, L_FL, 20))
# cut down to rim height except the snap flanges
lid = lid.cut(box(-1, L_XE + 1, L_Y - 20, L_Y + 20, L_RIM, L_FL + 1)
              .cut(box(FL_X0, FL_X1, L_Y - 20, L_Y - L_HW + FL_W, L_RIM - 1, L_FL + 2))
              .cut(box(FL_X0, FL_X1, L_Y + L_HW - FL_W, L_Y + 20, L_RIM - 1, L_FL + 2)))
# inner cavity
lid = lid.cut(d_prism(L_END0, L_X1, L_Y, L_HW - L_T, L_FL + 2, L_R - L_T, z0=L_T, fillet_ends=L_IN_R, ends=">X")
              .intersect(box(0, L_XE, L_Y - 20, L_Y + 20, 0, L_RIM + 0.01)))
# concave grooves on the inner faces of the flanges
for s in (-1, 1):
    yi = L_Y + s * (L_HW - FL_W)
    lid = lid.cut(cyl_x(FL_X0 - 0.1, FL_X1 + 0.1, yi - s * (GROOVE_R - GROOVE_D), GROOVE_Z, GROOVE_R))
# -X end wall: thinner in the middle
lid = lid.cut(box(L_END_THIN, L_END0 + 0.1, L_Y - L_END_HW, L_Y + L_END_HW, L_T, L_RIM + 1).intersect(
    d_prism(0, L_END0 + 0.1, L_Y, L_HW - L_T, L_FL + 2, L_R - L_T, z0=L_T)))
# ledges next to the -X end wall
for s in (-1, 1):
    lid = lid.union(box(L_END0 - 0.1, LEDGE_X1, L_Y + s * LEDGE_IN, L_Y + s * LEDGE_OUT, 0.5, LEDGE_Z)
                    .union(box(L_END0 - 0.1, LEDGE_X1, L_Y + s * LEDGE_IN, L_Y + s * 13, 0.5, L_RIM))
                    .intersect(lid_env))
# partition
lid = lid.union(box(PART_X0, PART_X1, L_Y - 12, L_Y + 12, 0.5, L_RIM).intersect(lid_env))
# small raised blocks near the +X end
for s in (-1, 1):
    lid = lid.union(box(BLK_X0, BLK_X1, L_Y + s * BLK_Y0, L_Y + s * BLK_Y1, 1.0, BLK_Z))
# snap hooks with lead-in ramps on the +X end wall, split by a central channel
for s in (-1, 1):
    y0, y1 = sorted((L_Y + s * CH_HW, L_Y + s * EW_BLK_HW))
    ramp = (cq.Workplane("XZ", origin=(0, y1, 0))
            .polyline([(L_X1, L_RIM - 0.5), (L_XE, L_RIM - 0.5), (L_XE, EW_RAMP_Z), (EW_RAMP_X1, EW_RAMP_Z),
                       (EW_RAMP_X0, EW_BLK_Z), (L_X1, EW_BLK_Z)]).close().extrude(y1 - y0))
    lid = lid.union(ramp.intersect(lid_env))
lid = lid.cut(box(CH_X0, L_XE + 1, L_Y - CH_HW, L_Y + CH_HW, -1, 6))
# chamfer the channel mouth at the end face over the full height
for s in (-1, 1):
    tri = (cq.Workplane("XY").polyline([(L_XE + 0.01, L_Y + s * (CH_HW + EW_BLK_CH + 0.01)),
                                        (L_XE + 0.01, L_Y + s * (CH_HW - 0.01)),
                                        (L_XE - EW_BLK_CH - 0.01, L_Y + s * (CH_HW - 0.01))])
           .close().extrude(8).translate((0, 0, -1)))
    lid = lid.cut(tri)
# slot and hole through the floor
lid = lid.cut(box(SLOT_X0, SLOT_X1, L_Y - SLOT_HW, L_Y + SLOT_HW, -1, 3))
lid = lid.cut(cq.Workplane("XY").center(HOLE_X, L_Y).circle(HOLE_D / 2).extrude(4).translate((0, 0, -1)))

# ================= HINGE STRAP =================
hinge = (cq.Workplane("YZ").workplane(offset=HINGE_X0).center(HINGE_Y, HINGE_Z)
         .ellipse(HINGE_A, HINGE_B).extrude(HINGE_X1 - HINGE_X0))

result = tray.union(lid).union(hinge)
